import cadquery as cq

# ---------------------------------------------------------------
# Global layout (X right, Y depth from front face Y=0 backwards, Z up)
# Four separate moulded parts laid out side by side in the XZ plane:
#   box (housing tube), lid, cover plate, clip bracket
# ---------------------------------------------------------------

# ---- housing box ----
BOX_W = 60.0          # outer width / height (square)
BOX_R = 9.5           # outer corner radius
BOX_T = 2.6           # wall thickness
BOX_D = 38.0          # depth along Y
LIP_F = 1.2           # front spigot depth
LIP_F_IN = 1.6        # front spigot inset
LIP_B = 1.3           # back step depth
LIP_B_IN = 1.6        # back step inset
BOSS_A = 11.0         # corner boss size
BOSS_D = 6.0          # corner boss depth
BOSS_D_LONG = 14.0    # lower -X boss runs deeper
BOSS_HOLE = 2.3
TAB_P = 5.5           # latch tab protrusion from side wall
TAB_Z0, TAB_Z1 = 15.0, 19.5
CLIP_P = 0.8          # clip protrusion on the +X wall
BOSS_HOLE_OFF = 8.5   # hole centre from outer edges

VENT_L = 9.5
VENT_W = 2.5
VENT_P = 5.2
VENT_PX = 4.6         # slot pitch across the top / bottom walls
VENT_Y1 = 12.8        # centre of front vent column (at the wall middle)
VENT_Y2 = 25.8        # centre of back vent column (at the wall middle)
VENT_K = 0.43         # chevron: slot moves forward this much per mm off-centre
VENTX_Y1 = 11.8       # side (-X) wall vent columns
VENTX_Y2 = 23.6
VENTX_K = 0.15

# ---- lid ----
LID_X = 61.0
LID_T = 5.1           # total thickness
WEB_Y0 = 2.8          # front face of the central web
WEB_Y1 = 3.6          # back face of the central web
LID_RIM = 1.8         # rim wall thickness
FR_W = 36.0           # inner square frame size
FR_T = 1.7
WIN_W, WIN_H = 14.4, 27.6
LID_BOSS_D = 4.7
LID_BOSS_X = (-11.6, 14.5)
LID_BOSS_Z = (-13.2, 13.2)
RIB_T = 1.2
LID_CH = 0.6          # chamfer on the lid's front outer edge

# ---- cover plate ----
PL_X, PL_Z = 58.75, 58.3
PL_W = 55.4
PL_R = 8.7
PL_T = 2.0
PL_HOLE = 2.8
PL_HOLE_OFF = 6.0
PL_WIN_W, PL_WIN_H = 19.0, 15.0
PL_WIN_DX = 3.9
KEY_D1, KEY_D2 = 4.7, 3.2   # keyhole circles

# ---- bracket ----
BR_Y_FRAME = 6.4      # front frame depth
BR_Y_WING = 3.4       # wing depth
BR_Y_BACK = 20.8      # back of tube
BR_PIN_END = 27.3
TUBE_X0, TUBE_X1 = -16.7, 17.6
TUBE_Z0, TUBE_Z1 = 36.0, 76.3
FR_Z0, FR_Z1 = 32.4, 76.8    # front frame outline
TUBE_R = 7.5
TUBE_T = 2.0
WING_X0, WING_X1 = -26.6, 27.3
WING_T = 3.1
WING_TOP_Z = 75.1
WING_BOT_Z = 40.0
PIN_D = 4.6
PIN_X = (-12.0, 14.5)
PIN_Z = (43.2, 69.7)


def xz_plane(y):
    """Workplane whose local (x, y) = global (X, Z); extrusion goes towards -Y."""
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))


def rrect(cx, cz, w, h, r, y0, y1):
    wp = xz_plane(y1).center(cx, cz).rect(w, h)
    s = wp.extrude(y1 - y0)
    if r > 0:
        s = s.edges("|Y").fillet(r)
    return s


def blk(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").add(
        cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, cq.Vector(x0, y0, z0)))


def ycyl(x, z, d, y0, y1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(d / 2.0, y1 - y0, cq.Vector(x, y0, z), cq.Vector(0, 1, 0)))


def slot_y(x, z, yc, length, width, axis):
    """Through-slot cutter elongated along Y; axis = 'X' or 'Z' is the wall normal."""
    if axis == "Z":
        wp = cq.Workplane("XY").workplane(offset=z - 5).center(x, yc)
        return wp.slot2D(length, width, angle=90).extrude(10)
    else:
        wp = cq.Workplane("YZ").workplane(offset=x - 5).center(yc, z)
        return wp.slot2D(length, width, angle=0).extrude(10)


def vent(x, z, yc, axis):
    """Rectangular through vent elongated along Y in a wall normal to 'axis'."""
    if axis == "Z":
        return blk(x - VENT_W / 2, x + VENT_W / 2, yc - VENT_L / 2, yc + VENT_L / 2, z - 5, z + 5)
    return blk(x - 5, x + 5, yc - VENT_L / 2, yc + VENT_L / 2, z - VENT_W / 2, z + VENT_W / 2)


# =================================================================
# HOUSING BOX
# =================================================================
def boss_profile(sx, sz, y0, y1):
    h = BOX_W / 2.0
    cx = sx * (h - BOSS_A / 2.0)
    cz = sz * (h - BOSS_A / 2.0)
    return rrect(cx, cz, BOSS_A, BOSS_A, 2.0, y0, y1)


def make_box():
    h = BOX_W / 2.0
    body = rrect(0, 0, BOX_W, BOX_W, BOX_R, LIP_F, BOX_D - LIP_B)
    front = rrect(0, 0, BOX_W - 2 * LIP_F_IN, BOX_W - 2 * LIP_F_IN,
                  BOX_R - LIP_F_IN, 0, LIP_F + 0.01)
    back = rrect(0, 0, BOX_W - 2 * LIP_B_IN, BOX_W - 2 * LIP_B_IN,
                 BOX_R - LIP_B_IN, BOX_D - LIP_B - 0.01, BOX_D)
    body = body.union(front).union(back)

    # inner cavity (through), leaving the four corner screw bosses
    cav = rrect(0, 0, BOX_W - 2 * BOX_T, BOX_W - 2 * BOX_T, BOX_R - BOX_T, -1, BOX_D + 1)
    keep = None
    for sx in (-1, 1):
        for sz in (-1, 1):
            depth = BOSS_D_LONG if (sx < 0 and sz < 0) else BOSS_D
            b = boss_profile(sx, sz, 0.6, depth)
            keep = b if keep is None else keep.union(b)
    cav = cav.cut(keep)
    body = body.cut(cav)
    # recess the boss faces slightly behind the front spigot
    body = body.cut(rrect(0, 0, BOX_W - 2 * BOX_T, BOX_W - 2 * BOX_T, BOX_R - BOX_T, -1, 0.6))
    for sx in (-1, 1):
        for sz in (-1, 1):
            body = body.cut(ycyl(sx * (h - BOSS_HOLE_OFF), sz * (h - BOSS_HOLE_OFF),
                                 BOSS_HOLE, -1.0, BOSS_D + 1))

    # latch tabs on the side walls next to the bosses
    for sx in (-1, 1):
        for sz in (-1, 1):
            xin = sx * (h - BOX_T)
            x0, x1 = sorted((xin + sx * 0.01, xin - sx * TAB_P))
            z0, z1 = sorted((sz * TAB_Z0, sz * TAB_Z1))
            body = body.union(blk(x0, x1, 7.0, 10.0, z0, z1))

    # vertical rib on the inner -X wall near the front
    body = body.union(blk(-h + BOX_T - 0.01, -h + BOX_T + 1.2, 4.0, 5.6, -16.0, 16.0))

    # snap hook on the -X wall above the long boss
    hook = blk(-h + BOX_T - 0.01, -h + BOX_T + 3.5, 11.0, 16.0, -17.5, -15.0)
    hook = hook.union(blk(-h + BOX_T - 0.01, -h + BOX_T + 1.5, 11.0, 16.0, -19.5, -15.0))
    body = body.union(hook)

    # vents: chevron pattern (slots further back towards the middle of each wall)
    cut = None
    for i in range(5):
        z = -10.4 + i * VENT_P
        s = vent(-h, z, VENTX_Y1 - VENTX_K * abs(z), "X")
        cut = s if cut is None else cut.union(s)
    for i in range(6):
        z = -13.0 + i * VENT_P
        cut = cut.union(vent(-h, z, VENTX_Y2 - VENTX_K * abs(z), "X"))
    for zw in (-h, h):
        # front column: 5 slots, back column: 6 slots, staggered
        for i in range(5):
            x = (i - 2) * VENT_PX
            cut = cut.union(vent(x, zw, VENT_Y1 - VENT_K * abs(x), "Z"))
        for i in range(6):
            x = (i - 2.5) * VENT_PX
            cut = cut.union(vent(x, zw, VENT_Y2 - VENT_K * abs(x), "Z"))
    # thin slots on the side walls
    for xw in (-h, h):
        for z in (18.6, -18.6):
            cut = cut.union(slot_y(xw, z, 15.0, 6.5, 0.9, "X"))
    body = body.cut(cut)

    # clip on the +X wall
    clip = blk(h - 0.5, h + CLIP_P, 1.5, 10.5, -10.5, 8.5)
    clip = clip.cut(blk(h - BOX_T - 1, h + 2.0, 5.5, 8.0, -7.0, 5.0))
    body = body.union(clip)
    return body


# =================================================================
# LID
# =================================================================
def make_lid():
    import math
    cx = LID_X
    hw = BOX_W / 2.0
    inner = hw - LID_RIM
    fh = FR_W / 2.0
    # outer rim wall (full thickness), small chamfer on the front outer edge
    lid = rrect(cx, 0, BOX_W, BOX_W, BOX_R, 0, LID_T).faces("<Y").chamfer(LID_CH)
    lid = lid.cut(rrect(cx, 0, BOX_W - 2 * LID_RIM, BOX_W - 2 * LID_RIM,
                        BOX_R - LID_RIM, -1, LID_T + 1))
    # small inner ledge at the front of the rim
    ledge = rrect(cx, 0, BOX_W - 2 * LID_RIM + 0.02, BOX_W - 2 * LID_RIM + 0.02,
                  BOX_R - LID_RIM, 0.9, WEB_Y0 + 0.01)
    ledge = ledge.cut(rrect(cx, 0, BOX_W - 2 * LID_RIM - 1.4, BOX_W - 2 * LID_RIM - 1.4,
                            BOX_R - LID_RIM - 0.7, 0, LID_T))
    lid = lid.union(ledge)
    # central web
    web = rrect(cx, 0, BOX_W - 2 * LID_RIM + 0.02, BOX_W - 2 * LID_RIM + 0.02,
                BOX_R - LID_RIM, WEB_Y0, WEB_Y1)
    lid = lid.union(web)

    # front side: square frame wall
    fr = rrect(cx, 0, FR_W, FR_W, 0.5, 0.6, WEB_Y0 + 0.01)
    fr = fr.cut(rrect(cx, 0, FR_W - 2 * FR_T, FR_W - 2 * FR_T, 0.3, -1, WEB_Y0 + 0.5))
    lid = lid.union(fr)
    # back side: raised central block
    lid = lid.union(rrect(cx, 0, FR_W, FR_W, 4.0, WEB_Y1 - 0.01, LID_T - 0.3))

    # ribs on both sides of the web
    for (y0, y1) in ((WEB_Y0 - 1.0, WEB_Y0 + 0.01), (WEB_Y1 - 0.01, LID_T - 0.3)):
        for dx in (-13.2, 0.0, 13.2):
            for sz in (-1, 1):
                z0, z1 = sorted((sz * (fh - 0.2), sz * (inner + 0.5)))
                lid = lid.union(blk(cx + dx - RIB_T / 2, cx + dx + RIB_T / 2, y0, y1, z0, z1))
        # diagonal ribs: top-right, bottom-right, bottom-left
        for (sx, sz) in ((1, 1), (1, -1), (-1, -1)):
            p0x, p0z = sx * (fh - 0.5), sz * 11.6
            p1x, p1z = sx * (inner + 0.5), sz * 18.6
            L = math.hypot(p1x - p0x, p1z - p0z)
            ang = math.degrees(math.atan2(p1z - p0z, p1x - p0x))
            r = (xz_plane(y1).center(cx + (p0x + p1x) / 2, (p0z + p1z) / 2)
                 .transformed(rotate=(0, 0, ang)).rect(L, RIB_T).extrude(y1 - y0))
            lid = lid.union(r)

    # bosses inside the front frame
    for bx in LID_BOSS_X:
        for bz in LID_BOSS_Z:
            lid = lid.union(ycyl(cx + bx, bz, LID_BOSS_D, 0.9, WEB_Y0 + 0.01))

    # window
    lid = lid.cut(blk(cx - WIN_W / 2, cx + WIN_W / 2, -1, LID_T + 1, -WIN_H / 2, WIN_H / 2))
    # small slot through the web next to the left rim
    lid = lid.cut(blk(cx - hw + 4.0, cx - hw + 5.2, -1, LID_T + 1, 9.5, 12.5))
    return lid


# =================================================================
# COVER PLATE
# =================================================================
def make_plate():
    p = rrect(PL_X, PL_Z, PL_W, PL_W, PL_R, 0, PL_T)
    h = PL_W / 2.0
    for sx in (-1, 1):
        for sz in (-1, 1):
            p = p.cut(ycyl(PL_X + sx * (h - PL_HOLE_OFF), PL_Z + sz * (h - PL_HOLE_OFF),
                           PL_HOLE, -1, PL_T + 1))
    # square window
    p = p.cut(blk(PL_X + PL_WIN_DX - PL_WIN_W / 2, PL_X + PL_WIN_DX + PL_WIN_W / 2,
                  -1, PL_T + 1, PL_Z + 0.6 - PL_WIN_H / 2, PL_Z + 0.6 + PL_WIN_H / 2))
    # keyhole on the left
    kx = PL_X - h + 7.0
    kz = PL_Z + 0.6
    p = p.cut(ycyl(kx, kz, KEY_D1, -1, PL_T + 1))
    p = p.cut(ycyl(kx - 2.5, kz, KEY_D2, -1, PL_T + 1))
    return p


# =================================================================
# BRACKET
# =================================================================
def make_bracket():
    # front frame body (same outline as tube)
    tw = TUBE_X1 - TUBE_X0
    th = TUBE_Z1 - TUBE_Z0
    tcx = (TUBE_X0 + TUBE_X1) / 2
    tcz = (TUBE_Z0 + TUBE_Z1) / 2
    frame = rrect(tcx, (FR_Z0 + FR_Z1) / 2, tw, FR_Z1 - FR_Z0, 4.6, 0, BR_Y_FRAME)
    # front window
    frame = frame.cut(blk(-12.0, 12.2, -1, BR_Y_FRAME + 1, WING_BOT_Z - WING_T, 68.2))
    # open the left side below the left plate (narrow bar remains)
    frame = frame.cut(blk(TUBE_X0 - 1, -12.0, -1, 3.0, 40.0 + 0.01, 54.9))

    # wings
    wings = blk(WING_X0, WING_X1, 0, BR_Y_WING, WING_TOP_Z - WING_T, WING_TOP_Z)
    wings = wings.union(blk(WING_X0, WING_X1, 0, BR_Y_WING, WING_BOT_Z - WING_T, WING_BOT_Z))
    # left plate with slot
    lp = blk(-19.2, -12.0, 0, BR_Y_FRAME, 54.9, WING_TOP_Z)
    lp = lp.cut(blk(-15.5, -13.7, -1, 4, 56.7, 61.3))
    # right vertical bar joining the wings
    rb = blk(12.2, 15.6, 0, BR_Y_WING, WING_BOT_Z - 0.1, WING_TOP_Z - 0.1)

    br = frame.union(wings).union(lp).union(rb)

    # slot in the left plate
    br = br.cut(blk(-15.5, -13.7, -1, 1.5, 56.7, 61.3))
    # top channel (pocket) on top of the frame
    br = br.cut(blk(-8.5, 8.3, -1, 3.0, 72.5, TUBE_Z1 + 1))

    # tube behind
    tube = rrect(tcx, tcz, tw, th, TUBE_R, BR_Y_FRAME - 0.01, BR_Y_BACK)
    tube = tube.cut(rrect(tcx, tcz, tw - 2 * TUBE_T, th - 2 * TUBE_T, TUBE_R - TUBE_T,
                          0, BR_Y_BACK - 2.0))
    # back wall opening
    tube = tube.cut(blk(-12.0, 12.2, 0, BR_Y_BACK + 1, 36.2, 68.2))
    # open underside between the side walls
    tube = tube.cut(blk(TUBE_X0 + TUBE_T, TUBE_X1 - TUBE_T, BR_Y_FRAME + 0.5, BR_Y_BACK + 1,
                        TUBE_Z0 - 1, TUBE_Z0 + TUBE_T + 0.01))
    # notch in -X side wall near the back
    tube = tube.cut(blk(TUBE_X0 - 1, TUBE_X0 + TUBE_T + 0.5, 10.0, BR_Y_BACK + 1, 47.5, 60.0))
    br = br.union(tube)

    # pins on the back face
    for px in PIN_X:
        for pz in PIN_Z:
            br = br.union(ycyl(px, pz, PIN_D, BR_Y_BACK - 0.5, BR_PIN_END - 1.2))
            br = br.union(ycyl(px, pz, PIN_D - 1.6, BR_PIN_END - 1.3, BR_PIN_END))
    # inner rod (lower-left pin continues inside the tube)
    br = br.union(ycyl(PIN_X[0], PIN_Z[0], PIN_D - 1.0, 14.0, BR_Y_BACK))

    return br


box = make_box()
lid = make_lid()
plate = make_plate()
bracket = make_bracket()

result = cq.Workplane("XY").add(cq.Compound.makeCompound(
    [box.val(), lid.val(), plate.val(), bracket.val()]))

VIEW = {"azimuth": 45, "elevation": 26}
